import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------
W = 600.0            # overall width  (X)
D = 600.0            # overall depth  (Y)
FOOT_H = 52.0        # underside of cabinet above floor
BODY_H = 470.0       # cabinet body height (below top plate)
PLATE_T = 19.0       # top plate thickness
PLATE_FIL = 5.0      # top plate upper edge round
R_CORNER = 40.0      # vertical corner radius of cabinet / plate
BODY_FIL = 4.0       # small round on the cabinet's bottom edge

BACK_RECESS = 4.0    # back panel set back from corner posts
FRAME_DEPTH = 5.0    # front frame set-back at the posts (slopes to flush at door)
DOOR_RECESS = 1.5    # front door leaf set back behind the frame edge
BACK_DOOR_RECESS = 4.0

DOOR_XL = -209.0     # front door left edge
DOOR_XR = 211.0      # front door right edge
DOOR_Z0 = 123.0      # door bottom (absolute Z)
DOOR_Z1 = 429.0      # door top (absolute Z)

VENT_HW = 78.0       # half width of vent grilles
VENT_Z0 = 201.0
VENT_Z1 = 353.0
VENT_PROUD = 7.0     # vent projects beyond the cabinet skin

HANDLE_X0 = 154.0
HANDLE_X1 = 191.0
HANDLE_Z0 = 251.0
HANDLE_Z1 = 304.0
HANDLE_PROUD = 4.0
LH_Y0 = -191.0       # left side grab handle (Y range / Z range)
LH_Y1 = -153.0
LH_Z0 = 263.0
LH_Z1 = 318.0

Z0 = FOOT_H
Z1 = FOOT_H + BODY_H
Z2 = Z1 + PLATE_T
HX = W / 2.0
HY = D / 2.0
POST = HX - R_CORNER   # where the corner posts start

CAST_X = 190.0
CAST_Y = 196.0
WHEEL_D = 44.0
WHEEL_W = 26.0
WHEEL_ZC = 31.0
GROOVE_W = 1.2       # engraved graphic line width
GROOVE_D = 0.8


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)).val())


def cyl_z(x, y, z0, h, d):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(d / 2.0).extrude(h).val())


def seg_grooves(plane, pts, closed, width, depth):
    """Thin engraved line following a polyline on a plane (plane normal = outward)."""
    segs = list(zip(pts[:-1], pts[1:]))
    if closed:
        segs.append((pts[-1], pts[0]))
    out = []
    for (a, b) in segs:
        L = math.hypot(b[0] - a[0], b[1] - a[1])
        ang = math.degrees(math.atan2(b[1] - a[1], b[0] - a[0]))
        s = (cq.Workplane(plane).center((a[0] + b[0]) / 2, (a[1] + b[1]) / 2)
             .slot2D(L + width, width, ang).extrude(-depth, both=False))
        s = s.translate(plane.zDir * 0.2)
        out.append(s.val())
    return out


def plane_at(name, offset):
    p = cq.Plane.named(name)
    return cq.Plane(origin=p.zDir * offset, xDir=p.xDir, normal=p.zDir)


# ---------------------------------------------------------------
# Cabinet body
# ---------------------------------------------------------------
body = (cq.Workplane("XY").workplane(offset=Z0)
        .rect(W, D).extrude(BODY_H)
        .edges("|Z").fillet(R_CORNER)
        .faces("<Z").edges().fillet(BODY_FIL)).val()

cuts = []

# --- front (-Y): frame around the door slopes back towards the posts/top
#     (set back FRAME_DEPTH under the top plate, flush at the door edge).
#     Built as a closed shell: planar faces + one ruled (twisted) wing face.
V = cq.Vector
yf, yb = -HY, -HY + FRAME_DEPTH
P1 = V(-POST, yf, DOOR_Z0)
P2 = V(DOOR_XL, yf, DOOR_Z0)
P3 = V(DOOR_XL, yf, DOOR_Z1)
P4 = V(POST, yf, DOOR_Z1)
P5 = V(POST, yf, Z1)
P6 = V(-POST, yf, Z1)
Q5 = V(POST, yb, Z1)
Q6 = V(-POST, yb, Z1)


def poly_face(*pts):
    return cq.Face.makeFromWires(cq.Wire.makePolygon(list(pts), close=True))


frame_faces = [poly_face(P1, P2, P3, P4, P5, P6), poly_face(P5, P6, Q6, Q5),
               poly_face(P4, P5, Q5), poly_face(P3, P4, Q5, Q6), poly_face(P1, P6, Q6),
               cq.Face.makeRuledSurface(cq.Edge.makeLine(P1, Q6), cq.Edge.makeLine(P2, P3))]
frame_cut = cq.Solid.makeSolid(cq.Shell.makeShell(frame_faces))
cuts.append(frame_cut)

# --- back (+Y): recessed panel and door
cuts.append(box(-POST, POST, HY - BACK_RECESS, HY + 1, Z0 - 1, Z1))
YBD = HY - BACK_RECESS - BACK_DOOR_RECESS
cuts.append(box(-DOOR_XR, -DOOR_XL, YBD, HY - BACK_RECESS + 0.5, DOOR_Z0, DOOR_Z1))

# --- left (-X): shallow V-shaped crease panel near the front post
lv = (cq.Workplane(plane_at("YZ", -HX))
      .polyline([(-POST, Z1), (LH_Y0, LH_Z1), (LH_Y0, LH_Z0), (-POST, Z0)]).close()
      .extrude(1.5).val())
cuts.append(lv)

# --- underside outline groove of the base pan
gw = 1.6
for (x0, x1, y0, y1) in ((-CAST_X, CAST_X, -CAST_Y - gw / 2, -CAST_Y + gw / 2),
                         (-CAST_X, CAST_X, CAST_Y - gw / 2, CAST_Y + gw / 2),
                         (CAST_X - gw / 2, CAST_X + gw / 2, -CAST_Y, CAST_Y)):
    cuts.append(box(x0, x1, y0, y1, Z0 - 1, Z0 + 1.0))

# door leaf sits slightly behind the frame
cuts.append(box(DOOR_XL, DOOR_XR, -HY - 1, -HY + DOOR_RECESS, DOOR_Z0, DOOR_Z1))
body = body.cut(*cuts)

# ---------------------------------------------------------------
# Right (+X) side: indicator brow, LEDs and logo
# ---------------------------------------------------------------
BROW_Z = 494.0
brow_pts = [(-258, Z1), (-258, Z1 - 1.5), (-121, BROW_Z), (121, BROW_Z), (258, Z1 - 1.5), (258, Z1)]
brow = (cq.Workplane(plane_at("YZ", HX - 0.5))
        .polyline(brow_pts).close().extrude(3.0)).val()

LOGO_Z = 300.0
LOGO_D = 84.0
logo = (cq.Workplane(plane_at("YZ", HX - 0.5))
        .center(0, LOGO_Z).circle(LOGO_D / 2).extrude(3.5)).val()
logo_cuts = [(cq.Workplane(plane_at("YZ", HX + 1.8))
              .center(0, LOGO_Z).circle(LOGO_D / 2 - 2).circle(LOGO_D / 2 - 5.5)
              .extrude(3)).val()]
# stylised "Ai" mark: two strokes of the A, the stem of the i and its dot
for (a, b) in (((-24.1, 286.0), (-8.8, 313.9)),
               ((-8.8, 313.9), (5.9, 286.7)),
               ((12.7, 303.0), (24.4, 286.7))):
    L = math.hypot(b[0] - a[0], b[1] - a[1])
    ang = math.degrees(math.atan2(b[1] - a[1], b[0] - a[0]))
    logo_cuts.append((cq.Workplane(plane_at("YZ", HX + 1.8))
                      .center((a[0] + b[0]) / 2, (a[1] + b[1]) / 2)
                      .slot2D(L + 6.0, 6.0, ang).extrude(3)).val())
logo_cuts.append((cq.Workplane(plane_at("YZ", HX + 1.8))
                  .center(8.2, 313.9).circle(2.4).extrude(3)).val())
logo = logo.cut(*logo_cuts)

body = body.fuse(brow, logo)
led_pts = [(-121.25 + 48.5 * k, BROW_Z) for k in range(6)]
leds = (cq.Workplane(plane_at("YZ", HX - 4))
        .pushPoints(led_pts).circle(6).extrude(10)).val()
body = body.cut(leds)

# ---------------------------------------------------------------
# Front (-Y) graphics: crease facet on the door, lightning on the strip
# ---------------------------------------------------------------
YD = -HY + DOOR_RECESS         # front door skin
facet = (cq.Workplane(plane_at("XZ", -YD - 0.3))  # XZ normal is -Y
         .polyline([(DOOR_XL, DOOR_Z1), (DOOR_XR, DOOR_Z1), (HANDLE_X1, HANDLE_Z1),
                    (HANDLE_X0, HANDLE_Z0), (VENT_HW, VENT_Z0), (-VENT_HW, VENT_Z0)])
         .close().extrude(1.3)).val()
body = body.fuse(facet)

strip_plane = plane_at("XZ", HY)
bolt2 = [(230.8, 251.4), (251.8, 243.0), (249.7, 224.0), (244.0, 214.0), (249.0, 204.0),
         (243.0, 194.0), (248.0, 184.0), (241.0, 172.0), (221.0, 80.0)]
front_gr = seg_grooves(strip_plane, bolt2, True, GROOVE_W, GROOVE_D)
# seam lines: right-hand post joint and the line below the door's right corner
front_gr += seg_grooves(strip_plane, [(POST - 0.6, Z0 - 2), (POST - 0.6, DOOR_Z1)], False,
                        GROOVE_W, GROOVE_D)
front_gr += seg_grooves(strip_plane, [(DOOR_XR, DOOR_Z0), (221.0, 80.0), (221.0, Z0 - 2)], False,
                        GROOVE_W, GROOVE_D)
body = body.cut(*front_gr)

# ---------------------------------------------------------------
# Top plate
# ---------------------------------------------------------------
plate = (cq.Workplane("XY").workplane(offset=Z1)
         .rect(W, D).extrude(PLATE_T)
         .edges("|Z").fillet(R_CORNER)
         .faces(">Z").edges().fillet(PLATE_FIL)).val()

pcuts = []
for sx in (-1, 1):
    for sy in (-1, 1):
        pcuts.append(cyl_z(sx * 257, sy * 257, Z2 - 8, 10, 6))


pcuts.append(cyl_z(-197, 121, Z2 - 12, 13, 48))   # large access port
pcuts.append(cyl_z(70, 210, Z2 - 10, 11, 31))
pcuts.append(cyl_z(70, -52, Z2 - 10, 11, 31))
pcuts.append(cyl_z(-197, -206, Z2 - 10, 11, 30))

# square service hatch (outline groove)
HATCH_C = (-194.0, 1.0)
HATCH_S = 139.0
pcuts.append((cq.Workplane("XY").workplane(offset=Z2 - 1.2)
              .center(*HATCH_C).rect(HATCH_S, HATCH_S).rect(HATCH_S - 3, HATCH_S - 3)
              .extrude(2)).val())

# power switch pocket
SW_C = (-113.0, -230.0)
pcuts.append((cq.Workplane("XY").workplane(offset=Z2 - 6)
              .center(*SW_C).rect(38, 51).extrude(7)).val())

# small holes next to the switch
for x in (-209, -188):
    for y in (-233, -254):
        pcuts.append(cyl_z(x, y, Z2 - 2, 3, 3))

# perforation grid
GRID_X = [56 + 40.6 * i for i in range(6)]
GRID_Y = [227.5 - 59.3 * j for j in range(7)]
present = {0: (0, 1, 2, 3, 5), 1: (0, 1, 2, 5), 2: (0, 1, 2), 3: (0, 1, 2),
           4: (0, 1, 2, 5), 5: (0, 1, 2, 3, 5), 6: (0, 1, 2, 3, 4, 5)}
grid_pts = [(GRID_X[i], GRID_Y[j]) for j in present for i in present[j]]
pcuts.append((cq.Workplane("XY").workplane(offset=Z2 - 2)
              .pushPoints(grid_pts).circle(1.6).extrude(3)).val())

# engraved lightning graphic
top_plane = plane_at("XY", Z2)
bolt = [(178.5, 168.5), (219.3, 168.5), (219.3, 50.0), (258.6, 50.0), (217.8, -10.5),
        (246.9, -23.7), (219.3, -67.7), (188.0, -30.0), (174.6, -22.2), (172.3, 32.7),
        (178.5, 50.0)]
pcuts += seg_grooves(top_plane, bolt, True, GROOVE_W, GROOVE_D)
pcuts += seg_grooves(top_plane, [(219.3, 109.8), (258.6, 109.8)], False, GROOVE_W, GROOVE_D)
pcuts += seg_grooves(top_plane, [(246.9, -23.7), (258.6, -67.7)], False, GROOVE_W, GROOVE_D)
pcuts += seg_grooves(top_plane, [(217.5, 228.0), (255.8, 290.0), (279.0, 287.0)], True,
                     GROOVE_W, GROOVE_D)

plate = plate.cut(*pcuts)
rocker = (cq.Workplane("XY").workplane(offset=Z2 - 6)
          .center(*SW_C).rect(28, 40).extrude(4.5)
          .edges("|Z").fillet(4)).val()
plate = plate.fuse(rocker)

# ---------------------------------------------------------------
# Grilles and handles
# ---------------------------------------------------------------
def slab_y(y_in, y_out, x0, x1, z0, z1):
    a, b = sorted((y_in, y_out))
    return box(x0, x1, a, b, z0, z1)


def louvre_vent_y(y_in, y_out, hw, z0, z1, n, open_frac):
    """Grille block on a Y-facing skin with n horizontal louvre slots."""
    sgn = 1 if y_out > y_in else -1
    blk = slab_y(y_in - sgn * 0.5, y_out, -hw, hw, z0, z1)
    m = 4.0
    pitch = (z1 - z0 - 2 * m) / n
    depth = abs(y_out - y_in) - 2.0
    pts = [(0.0, z0 + m + pitch * (k + 0.5)) for k in range(n)]
    # XZ workplane normal is -Y; place it on the outer face and cut inward
    pl = plane_at("XZ", -y_out - sgn * 0.5)
    slots = (cq.Workplane(pl).pushPoints(pts)
             .rect(2 * hw - 2 * m, pitch * open_frac)
             .extrude(sgn * (depth + 0.5))).val()
    return blk.cut(slots)


def handle_y(y_in, y_out, x0, x1, z0, z1):
    sgn = 1 if y_out > y_in else -1
    blk = slab_y(y_in - sgn * 0.5, y_out, x0, x1, z0, z1)
    pocket = slab_y(y_out + sgn * 1, y_out - sgn * 3.5, x0 + 7, x1 - 8, z0 + 8, z1 - 8)
    return blk.cut(pocket)


front_vent = louvre_vent_y(YD, -HY - VENT_PROUD, VENT_HW, VENT_Z0, VENT_Z1, 22, 0.55)
front_handle = handle_y(YD, -HY - HANDLE_PROUD, HANDLE_X0, HANDLE_X1, HANDLE_Z0, HANDLE_Z1)

back_grille = louvre_vent_y(YBD, HY + VENT_PROUD, VENT_HW, VENT_Z0, VENT_Z1, 40, 0.55)
back_handle = handle_y(YBD, HY + HANDLE_PROUD, HANDLE_X0, HANDLE_X1, HANDLE_Z0, HANDLE_Z1)
hinges = [box(-DOOR_XR - 4, -DOOR_XR + 6, YBD - 0.5, YBD + 7, zc - 17, zc + 17)
          for zc in (160.0, 392.0)]

# left (-X) perforated vent and grab handle
lv_blk = box(-HX - VENT_PROUD, -HX + 0.5, -VENT_HW, VENT_HW, VENT_Z0, VENT_Z1)
pitch = 7.0
ny = int((2 * VENT_HW - 10) // pitch)
nz = int((VENT_Z1 - VENT_Z0 - 10) // pitch)
lpts = [(-(ny - 1) * pitch / 2 + i * pitch,
         (VENT_Z0 + VENT_Z1) / 2 - (nz - 1) * pitch / 2 + k * pitch)
        for i in range(ny) for k in range(nz)]
lholes = (cq.Workplane(plane_at("YZ", -HX - VENT_PROUD - 1))
          .pushPoints(lpts).circle(2.2).extrude(VENT_PROUD)).val()
left_vent = lv_blk.cut(lholes)

lh_blk = box(-HX - HANDLE_PROUD, -HX + 0.5, LH_Y0, LH_Y1, LH_Z0, LH_Z1)
lh_pocket = box(-HX - HANDLE_PROUD - 1, -HX - HANDLE_PROUD + 3.5,
                LH_Y0 + 7, LH_Y1 - 8, LH_Z0 + 8, LH_Z1 - 8)
left_handle = lh_blk.cut(lh_pocket)

# ---------------------------------------------------------------
# Levelling feet and castors
# ---------------------------------------------------------------
FOOT_OFF = 253.0
FOOT_D = 71.0


def foot(x, y):
    pad = cyl_z(x, y, 0, 5, FOOT_D - 3).fuse(cyl_z(x, y, 4.5, 7.5, FOOT_D))   # rubber + metal disc
    cone = (cq.Workplane("XY").workplane(offset=12).center(x, y).circle(FOOT_D / 2)
            .workplane(offset=11).circle(22).loft()).val()
    nut = (cq.Workplane("XY").workplane(offset=27).center(x, y)
           .polygon(6, 21).extrude(8)).val()
    stem = cyl_z(x, y, 22, Z0 - 22 + 0.5, 12)
    return pad.fuse(cone, nut, stem)


def castor(x, y):
    wheel = (cq.Workplane(plane_at("XZ", -(y + WHEEL_W / 2)))
             .center(x, WHEEL_ZC).circle(WHEEL_D / 2).extrude(WHEEL_W)
             .faces("<Y or >Y").edges().fillet(3)).val()
    axle = (cq.Workplane(plane_at("XZ", -(y + WHEEL_W / 2 + 6)))
            .center(x, WHEEL_ZC).circle(5).extrude(WHEEL_W + 12)).val()
    fork_pts = [(x - 14, Z0 + 0.5), (x + 8, Z0 + 0.5), (x + 5, WHEEL_ZC), (x - 3, WHEEL_ZC - 5)]
    parts = [axle]
    for s in (-1, 1):
        yp = y + s * (WHEEL_W / 2 + 2.5)
        parts.append((cq.Workplane(plane_at("XZ", -(yp + 1.5)))
                      .polyline(fork_pts).close().extrude(3)).val())
    parts.append(box(x - 18, x + 10, y - 18, y + 18, Z0 - 3, Z0 + 0.5))
    return wheel.fuse(*parts)


adds = [plate, front_vent, front_handle, back_grille, back_handle, left_vent, left_handle]
adds += hinges
for sx in (-1, 1):
    for sy in (-1, 1):
        adds.append(foot(sx * FOOT_OFF, sy * FOOT_OFF))
        adds.append(castor(sx * CAST_X, sy * CAST_Y))

result = cq.Workplane("XY").add(body.fuse(*adds))

VIEW = {"azimuth": 45, "elevation": 26}
